"""Thin warped shim strip: a long rectangular sheet (L ~ 6.3 W) with a smooth
hump in the middle.  The hump is about twice as high along the front edge
(-Y) as along the back edge (+Y), so the two ends are slightly twisted, and the
sheet sags a little across its width at the crest.  Modelled as one smooth
B-spline sheet face (from the edge height tables) given a small thickness."""
import cadquery as cq
from OCP.Approx import Approx_IsoParametric
from OCP.BRepBuilderAPI import (BRepBuilderAPI_MakeEdge, BRepBuilderAPI_MakeFace,
                                BRepBuilderAPI_MakeWire)
from OCP.BRepLib import BRepLib
from OCP.GCE2d import GCE2d_MakeSegment
from OCP.GeomAPI import GeomAPI_PointsToBSplineSurface
from OCP.TColgp import TColgp_Array2OfPnt
from OCP.gp import gp_Pnt, gp_Pnt2d

# ---------------- driving dimensions (mm) ----------------
W = 32.0              # strip width (Y)
L = 6.345 * W         # strip length (X)
T = 0.10              # sheet thickness (thin shim stock)

# Height of the strip (z, in units of W) along its two long edges, sampled at
# stations x = XS * L.  The front edge (y = -W/2) carries the larger hump, the
# back edge (y = +W/2) a flatter one, so the strip is slightly warped/twisted.
XS = [-0.5, -0.375, -0.25, -0.125, 0.0, 0.125, 0.25, 0.375, 0.5]
ZF = [0.0, 0.0492, 0.1104, 0.1890, 0.2307, 0.2032, 0.1278, 0.0590, 0.0145]
ZB = [0.0483, 0.0787, 0.1131, 0.1476, 0.1623, 0.1465, 0.1084, 0.0705, 0.0440]
# across the width the sheet sags below the straight line joining the two
# edges, most where the hump is highest (slight anticlastic cross curvature)
SAG = 0.015
NY = 7                # grid rows across the width
NSTA = 24             # boundary stations along each long edge (meshing only)


def hump_weights():
    avg = [(a + b) / 2 for a, b in zip(ZF, ZB)]
    lin = [avg[0] + (avg[-1] - avg[0]) * (x - XS[0]) / (XS[-1] - XS[0]) for x in XS]
    hump = [a - l for a, l in zip(avg, lin)]
    hmax = max(hump)
    return [h / hmax for h in hump]


def z_at(i, s):
    """height of station i at fraction s across the width (0 front, 1 back)"""
    lin = ZF[i] + (ZB[i] - ZF[i]) * s
    return (lin - SAG * HW[i] * 4.0 * s * (1.0 - s)) * W


HW = hump_weights()

# smooth B-spline mid-surface through the station grid
grid = TColgp_Array2OfPnt(1, len(XS), 1, NY)
for i, fx in enumerate(XS):
    for j in range(NY):
        s = j / (NY - 1)
        grid.SetValue(i + 1, j + 1, gp_Pnt(fx * L, (s - 0.5) * W, z_at(i, s)))
api = GeomAPI_PointsToBSplineSurface()
api.Interpolate(grid, Approx_IsoParametric)
surf = api.Surface()             # u: along X (0..1), v: across Y (0..1)


def uv_edge(a, b):
    seg = GCE2d_MakeSegment(gp_Pnt2d(*a), gp_Pnt2d(*b)).Value()
    e = BRepBuilderAPI_MakeEdge(seg, surf).Edge()
    BRepLib.BuildCurves3d_s(e)
    return e


# trimmed face = whole strip; its long edges are carried as NSTA stations each
corners = ([(i / NSTA, 0.0) for i in range(NSTA + 1)]
           + [(1.0 - i / NSTA, 1.0) for i in range(NSTA + 1)] + [(0.0, 0.0)])
wb = BRepBuilderAPI_MakeWire()
for a, b in zip(corners[:-1], corners[1:]):
    wb.Add(uv_edge(a, b))
sheet = cq.Face(BRepBuilderAPI_MakeFace(surf, wb.Wire(), True).Face())

# give the sheet its thickness (straight down)
solid = cq.Solid.extrudeLinear(sheet, cq.Vector(0, 0, -T))

result = cq.Workplane("XY").add(solid)
